import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 95.0          # length along X
H = 62.2          # height along Z
D = 26.8          # depth along Y (closed front face at Y=0, open back at Y=D)
R = 5.0           # corner radius of the XZ outline
C = 3.0           # chamfer around the closed front face
TX = 2.0          # end wall thickness (+X / -X walls)
TZ = 1.6          # long wall thickness (+Z / -Z walls)
TF = 2.0          # floor (front plate) thickness
# lid rebate around the open rim (the wall is thinned on its inside)
RIM_X = 1.3       # remaining end wall thickness in the rebate
RIM_Z = 0.85      # remaining long wall thickness in the rebate
REB_Y = 20.5      # deep rebate start: long walls and corners (|Z| > REB_ZMIN)
REB_ZMIN = 22.0
REB_ZMIN_XL = 14.0  # on the upper part of the -X wall the deep rebate reaches lower
REB2_Y = 24.3     # shallow rebate start: all around the rim

# external bosses on the front face
BOSS_D = 6.0
BOSS_H = 4.0
BOSS_HOLE = 2.2
BOSS_X = (-26.7, 30.7)
BOSS_Z = (24.2, -24.3)

# internal board standoffs (tab shaped, rounded towards the board centre)
SO_X = (-39.3, 18.7)
SO_Z = (24.0, -24.0)
SO_W = 4.8
SO_H = 2.4
SO_HOLE = 1.5

# floor pockets on the inner face of the front plate
POCKET = dict(x=1.6, z=11.6, l=26.5, w=10.0, d=0.8)

# ports in the top (+Z) wall : X centre, Y centre
USBC = dict(x=-31.0, y=7.3, w=9.0, h=3.6, ch=0.35)
HDMI_X = (-16.3, -2.8)
HDMI_Y = 7.25
HDMI_REC = (11.6, 7.8, 0.8)   # recess w, h, depth
HDMI_HOLE = (7.2, 5.0, 3.3)   # top width, bottom width, height (trapezoid)
AUDIO = dict(x=11.4, y=8.75, d=6.7)
VENT_TOP = dict(x=27.2, y=12.4)
VENT_PITCH = 5.0
VENT_LEN = 6.0
VENT_W = 2.2

# openings in the +X wall : (y0, y1, z0, z1)
XP_OPEN = [
    (5.7, 21.1, 12.4, 25.8),    # USB upper
    (5.8, 21.1, -5.2, 7.8),     # USB lower
    (5.8, 19.5, -25.2, -9.4),   # Ethernet
]
XP_OPEN_R = 0.4               # corner radius of those openings

# lid catches on the inner face of the bottom (-Z) wall, inside the rim rebate
CATCH_X = ((18.5, 28.3), (-27.5, -17.0))
CATCH_Y = (REB_Y, D - 1.2)
# lid catches on the inner face of the top (+Z) wall
TCATCH_X = ((9.6, 20.3), (-15.6, -8.5))
TCATCH_DROP = 1.0
# two small ribs on the inner face of the bottom wall
RIB_X = (-1.9, 5.4)
RIB_Y = (16.2, 19.0)
RIB_W = 0.8
RIB_H = 0.7

# -X wall features
SD = dict(z0=-5.65, z1=6.2, x=5.7, y=4.5, ch=2.3)
LED_Z = (19.9, 15.9)
LED_Y = 5.6
LED_D = 1.4
VENT_SIDE = dict(y=12.3, z=-16.8)
SCALLOP = dict(z=1.4, r=7.8, depth=3.5)


def slot_solid(length, width, depth, angle_deg=0.0):
    """Stadium prism centred at the origin in XY, extruded along Z by depth (centred)."""
    return (cq.Workplane("XY").slot2D(length, width, angle_deg)
            .extrude(depth).translate((0, 0, -depth / 2.0))).val()


def rounded_box(lx, ly, lz, r):
    return cq.Workplane("XY").box(lx, ly, lz).edges("|Y").fillet(r)


def combine(shapes):
    return cq.Workplane("XY").newObject(list(shapes))


# ---------------- main shell ----------------
outer = rounded_box(L, D, H, R).translate((0, D / 2.0, 0))
outer = outer.faces("<Y").edges().chamfer(C)

T = 0.5 * (TX + TZ)
ci = C + T * math.sqrt(2.0) - T - TF     # inner chamfer keeping the wall even
cav_len = D + 5.0
inner = rounded_box(L - 2 * TX, cav_len, H - 2 * TZ, R - T).translate(
    (0, TF + cav_len / 2.0, 0))
inner = inner.faces("<Y").edges().chamfer(ci)
reb_len = D - REB_Y + 2.0
reb = rounded_box(L - 2 * RIM_X, reb_len, H - 2 * RIM_Z, R - RIM_Z).translate(
    (0, REB_Y + reb_len / 2.0, 0))
reb = reb.cut(cq.Workplane("XY").box(L + 2.0, reb_len + 2.0, 2 * REB_ZMIN)
              .translate((0, REB_Y + reb_len / 2.0, 0)))
reb_xl = (rounded_box(L - 2 * RIM_X, reb_len, H - 2 * RIM_Z, R - RIM_Z)
          .translate((0, REB_Y + reb_len / 2.0, 0))
          .intersect(cq.Workplane("XY").box(L / 2.0, reb_len + 2.0, H / 2.0 - REB_ZMIN_XL)
                     .translate((-L / 4.0 - 1.0, REB_Y + reb_len / 2.0,
                                 REB_ZMIN_XL + (H / 2.0 - REB_ZMIN_XL) / 2.0))))
reb2_len = D - REB2_Y + 2.0
reb2 = rounded_box(L - 2 * RIM_X, reb2_len, H - 2 * RIM_Z, R - RIM_Z).translate(
    (0, REB2_Y + reb2_len / 2.0, 0))
body = outer.cut(combine([inner.val(), reb.val(), reb_xl.val(), reb2.val()]))

# ---------------- added material: bosses and standoffs ----------------
adds = []
for bx in BOSS_X:
    for bz in BOSS_Z:
        adds.append(cq.Workplane("XZ", origin=(bx, 0.0, bz)).circle(BOSS_D / 2.0)
                    .extrude(BOSS_H).val())
zin = H / 2.0 - TZ
for sx in SO_X:
    for sz in SO_Z:
        sgn = 1.0 if sz > 0 else -1.0
        ln = zin - abs(sz) + 0.5
        tab = (cq.Workplane("XZ", origin=(sx, TF, sz))
               .circle(SO_W / 2.0).extrude(-SO_H))
        blk = (cq.Workplane("XY").box(SO_W, SO_H, ln)
               .translate((sx, TF + SO_H / 2.0, sz + sgn * ln / 2.0)))
        adds.append(tab.union(blk).val())
zbot = -H / 2.0 + TZ
for (xa, xb) in CATCH_X:
    cz0, cz1 = -H / 2.0 + 0.5, zbot + 0.2
    adds.append(cq.Workplane("XY").box(xb - xa, CATCH_Y[1] - CATCH_Y[0], cz1 - cz0)
                .translate(((xa + xb) / 2.0, (CATCH_Y[0] + CATCH_Y[1]) / 2.0,
                            (cz0 + cz1) / 2.0)).val())
for (xa, xb) in TCATCH_X:
    cz0, cz1 = H / 2.0 - TZ - TCATCH_DROP, H / 2.0 - 0.5
    adds.append(cq.Workplane("XY").box(xb - xa, CATCH_Y[1] - CATCH_Y[0], cz1 - cz0)
                .translate(((xa + xb) / 2.0, (CATCH_Y[0] + CATCH_Y[1]) / 2.0,
                            (cz0 + cz1) / 2.0)).val())
for ry in RIB_Y:
    adds.append(cq.Workplane("XY").box(RIB_X[1] - RIB_X[0], RIB_W, RIB_H + 0.5)
                .translate(((RIB_X[0] + RIB_X[1]) / 2.0, ry, zbot + (RIB_H - 0.5) / 2.0)).val())
body = body.union(combine(adds))

# ---------------- cutters ----------------
cuts = []
for bx in BOSS_X:
    for bz in BOSS_Z:
        cuts.append(cq.Workplane("XZ", origin=(bx, 0.5, bz)).circle(BOSS_HOLE / 2.0)
                    .extrude(BOSS_H + 1.0).val())
for sx in SO_X:
    for sz in SO_Z:
        cuts.append(cq.Workplane("XZ", origin=(sx, TF + SO_H + 0.1, sz))
                    .circle(SO_HOLE / 2.0).extrude(SO_H).val())

for pz in (POCKET["z"], -POCKET["z"]):
    cuts.append(cq.Workplane("XZ", origin=(POCKET["x"], TF + 1.0, pz))
                .slot2D(POCKET["l"], POCKET["w"]).extrude(1.0 + POCKET["d"]).val())

ztop = H / 2.0
cuts.append(slot_solid(USBC["w"], USBC["h"], 10.0).translate(
    cq.Vector(USBC["x"], USBC["y"], ztop)))
cuts.append(cq.Workplane("XY", origin=(USBC["x"], USBC["y"], ztop - USBC["ch"]))
            .slot2D(USBC["w"], USBC["h"]).workplane(offset=USBC["ch"] + 0.01)
            .slot2D(USBC["w"] + 2 * USBC["ch"] + 0.02, USBC["h"] + 2 * USBC["ch"] + 0.02)
            .loft().val())
for hx in HDMI_X:
    rw, rh, rd = HDMI_REC
    cuts.append(cq.Workplane("XY", origin=(hx, HDMI_Y, ztop - rd))
                .rect(rw, rh).extrude(rd + 1.0).edges("|Z").fillet(1.5).val())
    tw, bw, hh = HDMI_HOLE
    pts = [(-bw / 2.0, -hh / 2.0), (bw / 2.0, -hh / 2.0), (tw / 2.0, hh / 2.0), (-tw / 2.0, hh / 2.0)]
    cuts.append(cq.Workplane("XY", origin=(hx, HDMI_Y, ztop - 5.0))
                .polyline(pts).close().extrude(10.0).edges("|Z").fillet(0.7).val())
cuts.append(cq.Workplane("XY", origin=(AUDIO["x"], AUDIO["y"], ztop - 5.0))
            .circle(AUDIO["d"] / 2.0).extrude(10.0).val())
for i in (-1, 0, 1):
    for j in (-1, 0, 1):
        cuts.append(slot_solid(VENT_LEN, VENT_W, 10.0, 45.0).translate(
            cq.Vector(VENT_TOP["x"] + i * VENT_PITCH, VENT_TOP["y"] + j * VENT_PITCH, ztop)))

xr = L / 2.0
for (y0, y1, z0, z1) in XP_OPEN:
    cuts.append(cq.Workplane("YZ", origin=(xr - 5.0, (y0 + y1) / 2.0, (z0 + z1) / 2.0))
                .rect(y1 - y0, z1 - z0).extrude(10.0).edges("|X").fillet(XP_OPEN_R).val())

xl = -L / 2.0
sd_w = SD["x"] + 5.0
sd_cx = xl - 5.0 + sd_w / 2.0
sd_cz = (SD["z0"] + SD["z1"]) / 2.0
sd_h = SD["z1"] - SD["z0"]
cuts.append(cq.Workplane("XY").box(sd_w, SD["y"] + 5.0, sd_h)
            .translate((sd_cx, SD["y"] - (SD["y"] + 5.0) / 2.0, sd_cz)).val())
chs = SD["ch"]
cuts.append(cq.Workplane("XZ", origin=(0, chs, 0))
            .center(sd_cx, sd_cz).rect(sd_w, sd_h)
            .workplane(offset=chs + 0.01)
            .center(chs / 2.0, 0).rect(sd_w + chs, sd_h + 2 * chs)
            .loft().val())
sc_cy = D + SCALLOP["r"] - SCALLOP["depth"]
cuts.append(cq.Workplane("YZ", origin=(xl - 1.0, sc_cy, SCALLOP["z"]))
            .circle(SCALLOP["r"]).extrude(TX + 2.0).val())
for lz in LED_Z:
    cuts.append(cq.Workplane("YZ", origin=(xl - 2.0, LED_Y, lz)).circle(LED_D / 2.0)
                .extrude(5.0).val())
for i in (-1, 0, 1):
    for j in (-1, 0, 1):
        cuts.append(cq.Workplane("YZ", origin=(xl - 3.0, VENT_SIDE["y"] + i * VENT_PITCH,
                                               VENT_SIDE["z"] + j * VENT_PITCH))
                    .slot2D(VENT_LEN, VENT_W, 45.0).extrude(6.0).val())

body = body.cut(combine(cuts))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
